import cadquery as cq
import math

# =====================================================================
#  Street-light style lamp head cover (solid moulding with bottom pockets)
#  X: long axis (pole tube at x=0, nose at x=L), Y: width, Z: up (floor z=0)
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
L_TOTAL = 600.0
SHOULDER = 35.0            # horizontal extent of the rounded side shoulder

# tube (pole entry) sections: (x, half width, height)
TUBE = [(0.0, 37.0, 32.5), (80.0, 46.3, 37.4)]
TUBE_END_FILLET = 14.0     # rounds the collar at the tube/neck joint
TUBE_TIP_FILLET = 4.0
# neck sections (x, half width, height)
NECK = [(60.0, 41.9, 32.5), (290.0, 72.9, 35.3)]
# body (lamp head)
BODY_H = 40.0
BODY_SECTIONS = [          # (x, half width, shoulder extent)
    (262.0, 76.5, 35.0),
    (360.0, 85.5, 35.0),
    (450.0, 87.0, 36.0),
    (530.0, 77.5, 37.0),
    (600.0, 55.0, 38.0),
]
NOSE_FILLET = 13.0
BACK_FILLET = 14.0
NECK_BLEND = 10.0          # concave blend neck -> body

# top hex nut pockets (on the centre line)
HEX_X = (298.0, 550.0)
HEX_AF = 24.0              # across flats
HEX_DEPTH = 9.0
BOLT_D = 12.0              # through hole under each hex pocket

# side window in the neck (-Y side), open to the floor
WIN_X0, WIN_X1 = 131.0, 254.0
WIN_TOP = 20.5
WIN_FAR_Y = 20.0           # how far the window pocket reaches across (+Y)
WIN_BOSSES = [(150.0, 8.0), (246.0, -46.0)]   # screw bosses under the window roof
WIN_BOSS_D, WIN_BOSS_HOLE, WIN_BOSS_BOTTOM = 10.0, 4.0, 11.0

# floor pockets
RIM = 13.0                 # width of the floor rim left around the edge
NECK_RECESS = 4.0          # depth of the shallow floor recess in tube + neck
FRONT_RECESS = [           # (x, half width) of that recess
    (6.0, 27.5), (66.0, 34.5), (95.0, 33.5), (276.0, 58.0)]
BODY_RECESS = 9.0          # depth of the floor recess in the lamp body
BODY_RECESS_OUTLINE = [    # body outline (x, half width, shoulder) the recess follows
    (276.0, 77.0, 35.0), (360.0, 85.5, 35.0), (450.0, 87.0, 36.0),
    (530.0, 77.5, 38.0), (586.0, 62.0, 40.0)]
GEAR_X0, GEAR_X1 = 320.0, 525.0   # gear-tray pocket in the body floor
GEAR_HW = 52.0
GEAR_DEPTH = 20.0
GEAR_FILLET = 14.0
# saddle channel under the tube
SADDLE_X0, SADDLE_STEP, SADDLE_X1 = 6.0, 50.0, 128.0
SADDLE_R0, SADDLE_R1 = 20.0, 24.0

# small half-round screw notches on the floor edge
NOSE_NOTCH_Y = 18.0
NOSE_NOTCH_R, NOSE_NOTCH_CB_R, NOSE_NOTCH_CB_D = 3.1, 6.7, 5.0
TUBE_NOTCH_R = 4.0

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- helpers ----------------
def section(x, hw, h, a=SHOULDER):
    """Closed, mirror-symmetric smooth loop in plane X=x.  Its upper half is the
    cross-section (flat-ish top, elliptical shoulders); the mirrored lower
    half is trimmed away by the floor plane z=0."""
    a = min(a, hw - 2.0)
    c = hw - a
    top = []
    for ang in (0, 25, 50, 70):
        t = math.radians(ang)
        top.append((c + a * math.cos(t), h * math.sin(t)))
    top += [(c, h), (0.0, h), (-c, h)]
    for ang in (110, 130, 155):
        t = math.radians(ang)
        top.append((-c + a * math.cos(t), h * math.sin(t)))
    bot = [(y, -z) for (y, z) in reversed(top[1:])]
    pts = top + [(-hw, 0.0)] + bot
    # start the periodic curve at the bottom centre so that its seam lies far
    # below the floor plane (keeps booleans/fillets clean)
    k = pts.index((0.0, -h))
    pts = pts[k:] + pts[:k]
    e = cq.Edge.makeSpline([cq.Vector(x, y, z) for y, z in pts], periodic=True)
    return cq.Wire.assembleEdges([e])


def loft(secs, ruled=False):
    return cq.Workplane("XY").add(
        cq.Solid.makeLoft([section(*s) for s in secs], ruled))


def slab(z0, z1):
    return (cq.Workplane("XY")
            .box(2 * L_TOTAL, 400, z1 - z0, centered=(True, True, False))
            .translate((L_TOTAL / 2, 0, z0)))


# ---------------- outer envelope ----------------
# every lofted piece is rounded first (closed periodic edge loops fillet
# cleanly) and then trimmed to the floor plane before the pieces are fused
UPPER = slab(0.0, 200.0)

tube = loft([(x, hw, h) for x, hw, h in TUBE], ruled=True)
tube = tube.faces(">X").edges().fillet(TUBE_END_FILLET)
tube = tube.faces("<X").edges().fillet(TUBE_TIP_FILLET)
tube = tube.intersect(UPPER)

neck = loft([(x, hw, h) for x, hw, h in NECK], ruled=True).intersect(UPPER)

body = loft([(x, hw, BODY_H, a) for x, hw, a in BODY_SECTIONS])
body = body.faces(">X").edges().fillet(NOSE_FILLET)
body = body.faces("<X").edges().fillet(BACK_FILLET)
body = body.intersect(UPPER)

part = tube.union(neck).union(body)
# concave blend where the neck runs into the back of the lamp body
BX = BODY_SECTIONS[0][0]
part = (part.edges(cq.selectors.BoxSelector((BX - 12.0, -100, 0.5), (BX + 8.0, 100, 60)))
        .fillet(NECK_BLEND))

# ---------------- top hex pockets + bolt holes ----------------
for hx in HEX_X:
    hex_cut = (cq.Workplane("XY", origin=(hx, 0, BODY_H - HEX_DEPTH))
               .polygon(6, HEX_AF / math.cos(math.radians(30)))
               .extrude(HEX_DEPTH + 5))
    hole = (cq.Workplane("XY", origin=(hx, 0, -1))
            .circle(BOLT_D / 2).extrude(BODY_H + 2))
    part = part.cut(hex_cut).cut(hole)

# ---------------- floor recesses ----------------
# shallow recess under tube + neck (rim narrower around the tube)
front_rec = loft([(x, hw, 20.0, 18.0) for x, hw in FRONT_RECESS], ruled=True)
part = part.cut(front_rec.intersect(slab(-1.0, NECK_RECESS)))

body_rec = loft([(x, hw - RIM, 25.0, a) for x, hw, a in BODY_RECESS_OUTLINE])
part = part.cut(body_rec.intersect(slab(-1.0, BODY_RECESS)))

gear = (cq.Workplane("XY")
        .box(GEAR_X1 - GEAR_X0, 2 * GEAR_HW, GEAR_DEPTH + 1, centered=False)
        .translate((GEAR_X0, -GEAR_HW, -1.0))
        .edges("|X").edges(">Z").fillet(GEAR_FILLET))
part = part.cut(gear)

# saddle channel under the pole tube (stepped half-bore)
sad0 = (cq.Workplane("YZ", origin=(SADDLE_X0, 0, 0)).circle(SADDLE_R0)
        .extrude(SADDLE_STEP - SADDLE_X0))
sad1 = (cq.Workplane("YZ", origin=(SADDLE_STEP, 0, 0)).circle(SADDLE_R1)
        .extrude(SADDLE_X1 - SADDLE_STEP))
part = part.cut(sad0).cut(sad1)

# ---------------- side window in the neck ----------------
win = (cq.Workplane("XY")
       .box(WIN_X1 - WIN_X0, 150.0, WIN_TOP + 1, centered=False)
       .translate((WIN_X0, WIN_FAR_Y - 150.0, -1.0)))
part = part.cut(win)
for bx, by in WIN_BOSSES:
    boss = (cq.Workplane("XY", origin=(bx, by, WIN_BOSS_BOTTOM))
            .circle(WIN_BOSS_D / 2).extrude(WIN_TOP - WIN_BOSS_BOTTOM + 1.0))
    part = part.union(boss)
    part = part.cut(cq.Workplane("XY", origin=(bx, by, WIN_BOSS_BOTTOM - 1.0))
                    .circle(WIN_BOSS_HOLE / 2).extrude(WIN_TOP - WIN_BOSS_BOTTOM + 4.0))

# ---------------- half-round notches on the floor edge ----------------
for sy in (-NOSE_NOTCH_Y, NOSE_NOTCH_Y):
    cb = (cq.Workplane("YZ", origin=(L_TOTAL - NOSE_NOTCH_CB_D, sy, 0))
          .circle(NOSE_NOTCH_CB_R).extrude(NOSE_NOTCH_CB_D + 5))
    nh = (cq.Workplane("YZ", origin=(L_TOTAL - 30.0, sy, 0))
          .circle(NOSE_NOTCH_R).extrude(35.0))
    part = part.cut(cb).cut(nh)
tn = (cq.Workplane("YZ", origin=(-5.0, 0, 0)).circle(TUBE_NOTCH_R).extrude(20.0))
part = part.cut(tn)

result = part
